import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
BEND_R = 600.0          # centre-line radius of the bent tube (arc in the XY plane)
HALF_ANGLE = 5.5        # half of the bend angle (deg) -> tube ends at +/- this angle

TUBE_OD = 45.0          # tube outside diameter
TUBE_ID = 34.0          # tube bore (continues, still bent, through the end plates)

RING_OD = 66.6          # split collar outside diameter
RING_W = 7.0            # collar axial width
RING_IN = 20.0          # collar inner radius used for modelling (buried in tube wall)
SLOT_W = 2.9            # width of the split in each collar
KEY_DROP = 1.5          # the key sitting in each split stops this far below the rim
RING_ANGLES = [-4.51, 1.96]   # collar positions along the arc (deg, + = towards +X)
SLOT_OFFSETS = [0.0, 3.0]     # sideways (+Y) offset of each collar's split

PLATE_B = 120.0         # triangular end plate: base width
PLATE_T = 26.5          # top (truncated apex) width
PLATE_H = 80.0          # height
PLATE_TH = 17.35        # mean thickness (at the plate centre line)
PLATE_WEDGE = 1.15      # outer face is turned this much further than the inner face (deg)
                        # -> plate is thicker on the outside (+Y) of the bend
AXIS_H = 34.15          # tube axis height above plate base

BOLT_D_RIGHT = 6.8      # blind bolt holes square to the outer face, +X plate
BOLT_D_LEFT = 10.5      # the -X plate carries larger bolt holes
BOLT_SKIN = 0.15        # material left under each bolt hole at the inner face
BOLT_POS = [(-41.4, 8.9), (41.4, 8.9), (0.0, 71.0)]   # (y, z above base)

FOOT_D = 10.0           # blind holes in the plate underside
FOOT_DEPTH = 15.0
FOOT_Y = 25.0

# angular position of the (cosmetic) seams of the round faces, 0 = +Y, 90 = +Z
SEAM_OUT = -50.0
SEAM_IN = 130.0

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- helpers ----------------
ZAX = cq.Vector(0, 0, 1)
CENTRE = cq.Vector(0, -BEND_R, 0)     # bend centre; tube apex sits at the origin


def place_on_arc(shape, ang_deg):
    """shape is built at the arc apex (tangent +X); swing it about the bend centre.
    positive ang_deg moves it towards +X."""
    return shape.rotate(CENTRE, CENTRE + ZAX, -ang_deg)


def x_circle(radius, seam_deg, x0=0.0):
    """circle in a plane normal to X (centred on the X axis at x0) whose seam
    point sits at angle seam_deg (0 = +Y, 90 = +Z)"""
    w = cq.Wire.makeCircle(radius, cq.Vector(x0, 0, 0), cq.Vector(1, 0, 0))
    # makeCircle starts at +Z (90 deg); turn the start point to seam_deg
    return w.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), seam_deg - 90.0)


def bent_rod(radius, half_angle_deg, seam_deg):
    """solid round bar bent on BEND_R, symmetric about the apex"""
    s = cq.Solid.revolve(
        x_circle(radius, seam_deg), [], 2 * half_angle_deg, CENTRE, CENTRE + ZAX
    )
    # revolve sweeps from the apex towards -X; centre it on the apex
    return s.rotate(CENTRE, CENTRE + ZAX, -half_angle_deg)


# ---------------- bent tube (solid for now, bored at the end) ----------------
part = cq.Workplane("XY").add(bent_rod(TUBE_OD / 2.0, HALF_ANGLE, SEAM_OUT))

# ---------------- split collars (with a key in the split) ----------------
keys = []
for a, off in zip(RING_ANGLES, SLOT_OFFSETS):
    ring = cq.Workplane("XY").add(
        cq.Solid.extrudeLinear(
            x_circle(RING_OD / 2.0, SEAM_OUT, -RING_W / 2.0),
            [x_circle(RING_IN, SEAM_OUT, -RING_W / 2.0)],
            cq.Vector(RING_W, 0, 0),
        )
    )
    slot = cq.Workplane("XY").box(RING_W * 3, SLOT_W, RING_OD).translate(
        (0, off, RING_OD / 2.0 + 5.0)
    )
    ring = ring.cut(slot)
    part = part.union(cq.Workplane("XY").add(place_on_arc(ring.val(), a)))

    key_bot = TUBE_OD / 2.0 - 2.0                 # buried in the tube wall
    key_top = RING_OD / 2.0 - KEY_DROP
    key = cq.Workplane("XY").box(RING_W, SLOT_W, key_top - key_bot).translate(
        (0, off, (key_top + key_bot) / 2.0)
    )
    keys.append(place_on_arc(key.val(), a))

# ---------------- end plates ----------------
# local frame: inner face on x = 0, outward = +x, tube axis along x at y = z = 0
zb = -AXIS_H
zt = PLATE_H - AXIS_H
tw = math.tan(math.radians(PLATE_WEDGE))
t_neg = PLATE_TH - PLATE_B / 2.0 * tw          # thickness at the -Y end
t_pos = PLATE_TH + PLATE_B / 2.0 * tw          # thickness at the +Y end

# front outline (truncated triangle) pushed along x ...
front = (
    cq.Workplane("YZ", origin=(-1.0, 0, 0))
    .polyline(
        [
            (-PLATE_B / 2.0, zb),
            (PLATE_B / 2.0, zb),
            (PLATE_T / 2.0, zt),
            (-PLATE_T / 2.0, zt),
        ]
    )
    .close()
    .extrude(t_pos + 2.0)
)
# ... intersected with the wedge-shaped plan outline pushed along z
plan = (
    cq.Workplane("XY", origin=(0, 0, zb - 1.0))
    .polyline(
        [
            (0.0, -PLATE_B / 2.0 - 5.0),
            (t_neg - 5.0 * tw, -PLATE_B / 2.0 - 5.0),
            (t_pos + 5.0 * tw, PLATE_B / 2.0 + 5.0),
            (0.0, PLATE_B / 2.0 + 5.0),
        ]
    )
    .close()
    .extrude(PLATE_H + 2.0)
)
plate_body = front.intersect(plan)


wa = math.radians(PLATE_WEDGE)
# drilling plane: parallel to the wedged outer face, 1 mm outside it
outer_pl = cq.Plane(
    origin=(PLATE_TH + 1.0 * math.cos(wa), -1.0 * math.sin(wa), 0),
    xDir=(math.sin(wa), math.cos(wa), 0),
    normal=(math.cos(wa), -math.sin(wa), 0),
)


def make_plate(bolt_d):
    plate = plate_body
    # blind bolt holes drilled square to the outer face; they stop just short of
    # the inner face, leaving a thin skin there
    for (y, z) in BOLT_POS:
        depth = (PLATE_TH + y * tw) / math.cos(wa) - BOLT_SKIN
        plate = plate.cut(
            cq.Workplane(outer_pl)
            .center((y + math.sin(wa)) / math.cos(wa), zb + z)
            .circle(bolt_d / 2.0)
            .extrude(-(depth + 1.0))
        )
    # blind holes in the underside, on the plate mid-thickness
    plate = plate.cut(
        cq.Workplane("XY", origin=(0, 0, zb - 1))
        .pushPoints([((PLATE_TH + y * tw) / 2.0, y) for y in (-FOOT_Y, FOOT_Y)])
        .circle(FOOT_D / 2.0)
        .extrude(FOOT_DEPTH + 1)
    )
    return plate.val()


th = math.radians(HALF_ANGLE)
end_pt = cq.Vector(BEND_R * math.sin(th), -BEND_R + BEND_R * math.cos(th), 0)
right_plate = make_plate(BOLT_D_RIGHT).rotate(cq.Vector(0, 0, 0), ZAX, -HALF_ANGLE).translate(end_pt)
left_plate = (
    make_plate(BOLT_D_LEFT)
    .rotate(cq.Vector(0, 0, 0), ZAX, -HALF_ANGLE)
    .translate(end_pt)
    .mirror("YZ", (0, 0, 0))
)

part = part.union(cq.Workplane("XY").add(right_plate)).union(
    cq.Workplane("XY").add(left_plate)
)

# ---------------- bent bore through tube and both plates ----------------
bore_half = math.degrees(math.asin((BEND_R * math.sin(th) + PLATE_TH * 2.0) / BEND_R))
part = part.cut(cq.Workplane("XY").add(bent_rod(TUBE_ID / 2.0, bore_half, SEAM_IN)))

# keys are separate inserts: fuse them without merging the coplanar faces so the
# split stays visible as edges on the collar faces
for k in keys:
    part = part.union(cq.Workplane("XY").add(k), clean=False)

result = part
